import math
import cadquery as cq

# ------------------------------------------------------------------ dimensions
H = 19.3             # overall height of the tray
T = 2.0              # wall thickness
FLOOR = 6.4          # floor thickness (top of floor above the underside)

W = 237.5            # overall width (X)
Y_LEFT = 139.7       # depth of the left (low) section
X_STEP = 78.0        # x of the step in the rear edge
Y_MID = 164.6        # depth of the middle section
X_SLANT = 177.3      # start of the slanted rear edge rising to the peak
PEAK = (201.4, 179.5)  # rear-right peak of the outline (virtual sharp corner)
PEAK_ANGLE = 32.0    # deg from +Y of the right-side curve where it meets the peak

# front-left sweep of the front edge (circular arc blending into the front)
X_FRONT_ARC = 47.0
R_FRONT_ARC = 128.0

# right side: straight at x=W, then curving round to the peak
RIGHT_CURVE = [(236.8, 100.0), (234.2, 115.0), (228.5, 131.0),
               (220.4, 146.5), (211.1, 162.0)]

# plan-view corner radii
R_FRONT_RIGHT = 4.0
R_FRONT_LEFT = 4.0
R_REAR_LEFT = 4.5
R_STEP = 3.0
R_PEAK = 3.0
R_INNER = 2.8        # minimum radius of the inside corners of the cavity

# edge rounds
R_TOP_EDGE = 0.8
R_BOT_EDGE = 1.2

# shallow pocket in the floor (front right)
POCKET_X0, POCKET_X1 = 168.6, 228.5
POCKET_Y0, POCKET_Y1 = 11.2, 108.9
POCKET_DEPTH = 4.8

# screw bosses
BOSS_POS = [(34.7, 42.6), (34.7, 104.6), (158.6, 38.4), (158.6, 100.8),
            (198.8, 128.5)]
BOSS_D = 8.2
BOSS_H = 10.0        # main cylinder height above the floor
BOSS_TOP_D = 5.4
BOSS_TOP_H = 2.3     # stepped spigot on top of the boss
BOSS_HOLE_D = 3.3
BOSS_HOLE_DEPTH = 9.0

# small notch in the top of the front wall
NOTCH_X = 198.3
NOTCH_W = 4.5
NOTCH_DEPTH = 6.2


# ------------------------------------------------------------------ outline
def _unit(x, y):
    l = math.hypot(x, y)
    return (x / l, y / l)


def _left(u):
    return (-u[1], u[0])


def _offset_vertex(v, uin, uout, off):
    """Vertex of the outline shifted inward by off (edges parallel)."""
    if not off:
        return v
    n1, n2 = _left(uin), _left(uout)
    k = off / (1.0 + n1[0] * n2[0] + n1[1] * n2[1])
    return (v[0] + k * (n1[0] + n2[0]), v[1] + k * (n1[1] + n2[1]))


def _corner(v, uin, uout, r):
    """Tangent points and arc mid point of a plan fillet of radius r at v."""
    if r <= 1e-6:
        return v, v, None
    cross = uin[0] * uout[1] - uin[1] * uout[0]
    dot = uin[0] * uout[0] + uin[1] * uout[1]
    d = r * math.tan(math.atan2(abs(cross), dot) / 2)
    t1 = (v[0] - d * uin[0], v[1] - d * uin[1])
    t2 = (v[0] + d * uout[0], v[1] + d * uout[1])
    nrm = _left(uin) if cross > 0 else (uin[1], -uin[0])
    c = (t1[0] + r * nrm[0], t1[1] + r * nrm[1])
    mx, my = _unit(t1[0] + t2[0] - 2 * c[0], t1[1] + t2[1] - 2 * c[1])
    return t1, t2, (c[0] + r * mx, c[1] + r * my)


def _radius(r, off, convex=True):
    """Corner radius of the parallel outline."""
    if not off or r <= 0:
        return r
    return max(r - off, R_INNER) if convex else r + off


def outline_wire(off=0.0):
    """Plan outline of the tray (counter-clockwise); off > 0 gives the inner
    outline of the cavity, parallel to the outer one at distance off."""
    V = cq.Vector
    edges = []

    def line(a, b):
        edges.append(cq.Edge.makeLine(V(a[0], a[1], 0), V(b[0], b[1], 0)))

    def arc(a, m, b):
        edges.append(cq.Edge.makeThreePointArc(V(a[0], a[1], 0), V(m[0], m[1], 0),
                                               V(b[0], b[1], 0)))

    # front-left: left side x=off blends (fillet) into the big front arc
    cbx, cby = X_FRONT_ARC, R_FRONT_ARC          # centre of the front arc
    ra = R_FRONT_ARC - off
    rf = _radius(R_FRONT_LEFT, off)
    fcx = off + rf
    fcy = cby - math.sqrt((ra - rf) ** 2 - (cbx - fcx) ** 2)
    p_left = (off, fcy)
    k = ra / (ra - rf)
    p_arc = (cbx + (fcx - cbx) * k, cby + (fcy - cby) * k)
    mx, my = _unit(p_left[0] + p_arc[0] - 2 * fcx, p_left[1] + p_arc[1] - 2 * fcy)
    arc(p_left, (fcx + rf * mx, fcy + rf * my), p_arc)
    a1 = math.atan2(p_arc[1] - cby, p_arc[0] - cbx)
    a2 = -math.pi / 2
    am = (a1 + a2) / 2
    p_front = (X_FRONT_ARC, off)
    arc(p_arc, (cbx + ra * math.cos(am), cby + ra * math.sin(am)), p_front)

    # front-right corner
    rr = _radius(R_FRONT_RIGHT, off)
    t1, t2, m = _corner(_offset_vertex((W, 0.0), (1, 0), (0, 1), off), (1, 0), (0, 1), rr)
    line(p_front, t1)
    arc(t1, m, t2)
    right_start = t2

    # peak and the rear edge
    th = math.radians(PEAK_ANGLE)
    u_peak = (-math.sin(th), math.cos(th))
    rear = [PEAK, (X_SLANT, Y_MID), (X_STEP, Y_MID), (X_STEP, Y_LEFT), (0.0, Y_LEFT),
            (0.0, 0.0)]
    radii = [(R_PEAK, True), (0.0, False), (R_STEP, True), (R_STEP, False),
             (R_REAR_LEFT, True)]
    dirs = [u_peak] + [_unit(b[0] - a[0], b[1] - a[1]) for a, b in zip(rear[:-1], rear[1:])]
    rear_corners = []
    for i in range(5):
        v = _offset_vertex(rear[i], dirs[i], dirs[i + 1], off)
        r = _radius(radii[i][0], off, radii[i][1])
        rear_corners.append(_corner(v, dirs[i], dirs[i + 1], r))

    # right side: straight, then sweeping round to the peak (spline)
    outer_pts = [(W, 40.0), (W, 75.0)] + RIGHT_CURVE
    pts = outer_pts
    if off:
        ref = cq.Edge.makeSpline([V(x, y, 0) for x, y in [(W, 0.0)] + outer_pts + [PEAK]],
                                 tangents=[V(0, 1, 0), V(u_peak[0], u_peak[1], 0)])
        samples = [ref.positionAt(j / 1000.0, "parameter") for j in range(1001)]
        pts = []
        for (x, y) in outer_pts:
            j = min(range(1001), key=lambda q: (samples[q].x - x) ** 2 + (samples[q].y - y) ** 2)
            tg = ref.tangentAt(j / 1000.0, "parameter")
            nx, ny = _left(_unit(tg.x, tg.y))
            pts.append((x + off * nx, y + off * ny))
    pts = [right_start] + pts + [rear_corners[0][0]]
    edges.append(cq.Edge.makeSpline([V(x, y, 0) for x, y in pts],
                                    tangents=[V(0, 1, 0), V(u_peak[0], u_peak[1], 0)]))

    # rear edge with its corners, then down the left side
    for i, (c1, c2, m) in enumerate(rear_corners):
        if m is not None:
            arc(c1, m, c2)
        nxt = rear_corners[i + 1][0] if i + 1 < len(rear_corners) else p_left
        line(c2, nxt)
    return cq.Wire.assembleEdges(edges)


outer_wire = outline_wire()
outer_face = cq.Face.makeFromWires(outer_wire)

# main body: extruded outline with rounded top and bottom outer edges
body = cq.Workplane("XY").add(cq.Solid.extrudeLinear(outer_face, cq.Vector(0, 0, H)))
body = body.faces(">Z").edges().fillet(R_TOP_EDGE)
body = body.faces("<Z").edges().fillet(R_BOT_EDGE)

# tray cavity (uniform wall thickness)
inner_wire = outline_wire(T)
cavity = cq.Solid.extrudeLinear(cq.Face.makeFromWires(inner_wire),
                                cq.Vector(0, 0, H + 2)).translate(cq.Vector(0, 0, FLOOR))
body = body.cut(cq.Workplane("XY").add(cavity))

# shallow rectangular pocket in the floor
pocket = (cq.Workplane("XY")
          .box(POCKET_X1 - POCKET_X0, POCKET_Y1 - POCKET_Y0, POCKET_DEPTH + 1,
               centered=False)
          .translate((POCKET_X0, POCKET_Y0, FLOOR - POCKET_DEPTH)))
body = body.cut(pocket)

# stepped screw bosses with pilot holes
for (bx, by) in BOSS_POS:
    boss = (cq.Workplane("XY").workplane(offset=FLOOR - 0.5).center(bx, by)
            .circle(BOSS_D / 2).extrude(BOSS_H + 0.5)
            .faces(">Z").workplane().circle(BOSS_TOP_D / 2).extrude(BOSS_TOP_H))
    body = body.union(boss)
    top_z = FLOOR + BOSS_H + BOSS_TOP_H
    hole = (cq.Workplane("XY").workplane(offset=top_z - BOSS_HOLE_DEPTH)
            .center(bx, by).circle(BOSS_HOLE_D / 2).extrude(BOSS_HOLE_DEPTH + 1))
    body = body.cut(hole)

# notch in the top of the front wall
notch = (cq.Workplane("XY")
         .box(NOTCH_W, T + 4, NOTCH_DEPTH + 1, centered=(True, False, False))
         .translate((NOTCH_X, -2, H - NOTCH_DEPTH)))
body = body.cut(notch)

result = body
